import math
import cadquery as cq

# =====================================================================
#  Team badge: square plate with raised "G + lightning bolt" logo and
#  raised lettering  "拱中航模队"  /  "GZ Aeromodelling team"
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 100.0      # plate width  (X)
PLATE_Y = 112.7      # plate depth  (Y)
PLATE_T = 4.3        # plate thickness

RING_H = 5.0         # height of the "G" ring layer above the plate
BOLT_H = 7.6         # height of the lightning bolt above the plate

G_CX, G_CY = -1.9, 9.8   # centre of the G ring
G_RO = 43.25             # outer radius
G_RI = 32.1              # inner radius
BAR_TOP = 9.75           # G cross-bar top edge (y)
BAR_BOT = -1.0           # G cross-bar bottom edge (y)
TERM_OUT = (32.72, 35.84)  # G upper terminal, outer corner
TERM_IN = (22.96, 30.20)   # G upper terminal, inner corner

# lightning bolt outline  A, B, C, D, E, F
BOLT = [(-43.15, 41.39), (21.4, 19.1), (6.45, 7.02), (38.0, -18.3),
        (-23.92, 2.64), (-9.26, 14.92)]
# lower "shadow" layer of the bolt (ring height)
SH_N = (-39.1, 32.1)       # spike root on the outer circle
SH_T1 = (-32.79, 17.21)    # crescent chord, upper end
SH_T2 = (-16.54, -16.87)   # crescent chord, lower end
SH_T3X = -5.21             # x where the shadow leaves the bolt edge E-D
SH_GAP = 0.37              # ledge of the shadow along bolt edge E-D
SH_LEDGE_X = 25.0          # ledge runs up to here (inside the ring)

# Chinese lettering (thin strokes)
CN_H = 3.9           # height above plate
CN_W = 0.8           # stroke width
CN_X0, CN_Y0 = -37.5, -48.6   # origin of the glyph data below
CN_SCALE = 1.0

# English lettering (bold strokes)
EN_H = 2.0           # height above plate
EN_W = 0.9           # stroke width
EN_BASE = -54.95     # baseline (y)
EN_CAP = 5.0         # cap / ascender height
EN_XH = 3.5          # x-height
EN_DESC = 1.1        # descender depth


def extrude_poly(pts, h, z0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(pts).close().extrude(h))


z0 = PLATE_T

# ---------------- plate ----------------
plate = cq.Workplane("XY").rect(PLATE_X, PLATE_Y).extrude(PLATE_T)

# ---------------- G ring layer ----------------
ring = (cq.Workplane("XY").workplane(offset=z0).center(G_CX, G_CY)
        .circle(G_RO).circle(G_RI).extrude(RING_H))

# opening of the G between cross-bar and upper terminal
dx, dy = TERM_OUT[0] - TERM_IN[0], TERM_OUT[1] - TERM_IN[1]
L = math.hypot(dx, dy)
ux, uy = dx / L, dy / L
p_in = (TERM_IN[0] - 6 * ux, TERM_IN[1] - 6 * uy)
p_out = (TERM_OUT[0] + 20 * ux, TERM_OUT[1] + 20 * uy)
cut_pts = [p_in, p_out, (70.0, p_out[1]), (70.0, BAR_TOP), (p_in[0], BAR_TOP)]
ring = ring.cut(extrude_poly(cut_pts, RING_H + 2, z0 - 1))

# cross bar of the G
bar = (cq.Workplane("XY").workplane(offset=z0)
       .center((8.0 + 50.0) / 2, (BAR_TOP + BAR_BOT) / 2)
       .rect(50.0 - 8.0, BAR_TOP - BAR_BOT).extrude(RING_H))
disk = (cq.Workplane("XY").workplane(offset=z0).center(G_CX, G_CY)
        .circle(G_RO).extrude(RING_H))
bar = bar.intersect(disk)

# shadow polygon of the bolt at ring height; along the lower bolt edge E-D
# it stands out by a narrow ledge SH_GAP
A, B, C, D, E, F = BOLT
edx, edy = D[0] - E[0], D[1] - E[1]
edl = math.hypot(edx, edy)
nx, ny = edy / edl, -edx / edl          # outward normal of edge E-D


def on_ed(x, off=0.0):
    y = E[1] + (x - E[0]) / edx * edy
    return (x + off * nx, y + off * ny)


T3 = on_ed(SH_T3X, SH_GAP)
ex, ey = SH_T1[0] - SH_T2[0], SH_T1[1] - SH_T2[1]
T1x = (SH_T1[0] + 0.15 * ex, SH_T1[1] + 0.15 * ey)
shadow = extrude_poly([SH_N, A, F, E, on_ed(SH_LEDGE_X), on_ed(SH_LEDGE_X, SH_GAP),
                       T3, SH_T2, T1x], RING_H, z0)

# lightning bolt: lower part belongs to the ring layer, upper part stands
# proud of it (kept as separate wall faces, like the original model)
bolt_low = extrude_poly(BOLT, RING_H, z0)
bolt_top = extrude_poly(BOLT, BOLT_H - RING_H, z0 + RING_H)

logo = ring.union(bar).union(shadow).union(bolt_low)
body = plate.union(logo)


# =====================================================================
#  lettering helpers: every stroke is a centre-line path (lines / arcs);
#  each segment becomes a band of the stroke width (rectangle or annular
#  sector) with round joints, all fused and extruded as plain prisms
# =====================================================================
def V(p):
    return cq.Vector(p[0], p[1], 0)


def circ3(p0, pm, p1):
    """centre and radius of the circle through three points"""
    ax, ay = p0
    bx, by = pm
    cx, cy = p1
    d = 2 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay)
          + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx)
          + (cx * cx + cy * cy) * (bx - ax)) / d
    return (ux, uy), math.hypot(ax - ux, ay - uy)


def radial(c, p, d):
    vx, vy = p[0] - c[0], p[1] - c[1]
    n = math.hypot(vx, vy)
    return (p[0] + d * vx / n, p[1] + d * vy / n)


def line_face(p0, p1, w):
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    n = math.hypot(dx, dy)
    nx, ny = -dy / n * w / 2, dx / n * w / 2
    pts = [(p0[0] + nx, p0[1] + ny), (p1[0] + nx, p1[1] + ny),
           (p1[0] - nx, p1[1] - ny), (p0[0] - nx, p0[1] - ny)]
    return cq.Face.makeFromWires(cq.Wire.makePolygon([V(p) for p in pts], close=True))


def arc_face(p0, pm, p1, w):
    c, r = circ3(p0, pm, p1)
    o0, om, o1 = radial(c, p0, w / 2), radial(c, pm, w / 2), radial(c, p1, w / 2)
    i0, im, i1 = radial(c, p0, -w / 2), radial(c, pm, -w / 2), radial(c, p1, -w / 2)
    edges = [cq.Edge.makeThreePointArc(V(o0), V(om), V(o1)),
             cq.Edge.makeLine(V(o1), V(i1)),
             cq.Edge.makeThreePointArc(V(i1), V(im), V(i0)),
             cq.Edge.makeLine(V(i0), V(o0))]
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


def path_faces(segs, w, caps=True):
    """faces of one stroke: segment bodies plus round joints / caps"""
    faces = []
    joints = []
    for s in segs:
        if s[0] == "L":
            faces.append(line_face(s[1], s[2], w))
            joints += [s[1], s[2]]
        else:
            faces.append(arc_face(s[1], s[2], s[3], w))
            joints += [s[1], s[3]]
    ends = (joints[0], joints[-1])
    seen = []
    for j in joints:
        if any(abs(j[0] - q[0]) < 1e-6 and abs(j[1] - q[1]) < 1e-6 for q in seen):
            continue
        seen.append(j)
        is_end = j in ends and joints.count(j) == 1
        if caps or not is_end:
            faces.append(dot_face(j, w / 2))
    return faces


def poly_faces(pts, w, caps=True):
    segs = [("L", pts[i], pts[i + 1]) for i in range(len(pts) - 1)]
    return path_faces(segs, w, caps)


def ring_face(c, r, w):
    o = cq.Wire.makeCircle(r + w / 2, V(c), cq.Vector(0, 0, 1))
    i = cq.Wire.makeCircle(r - w / 2, V(c), cq.Vector(0, 0, 1))
    return cq.Face.makeFromWires(o, [i])


def dot_face(c, r):
    return cq.Face.makeFromWires(cq.Wire.makeCircle(r, V(c), cq.Vector(0, 0, 1)))


def faces_to_solid(faces, h, z):
    sols = [cq.Solid.extrudeLinear(f, cq.Vector(0, 0, h)) for f in faces]
    s = sols[0]
    if len(sols) > 1:
        s = s.fuse(*sols[1:]).clean()
    return s.translate(cq.Vector(0, 0, z))


# ---------------- Chinese characters (stroke centre lines, mm) ----------
CN_GLYPHS = [
    # 拱
    [[(0.11, 10.08), (5.00, 10.08)],
     [(2.85, 13.40), (2.85, 1.66), (1.28, 2.25)],
     [(0.30, 5.77), (5.00, 8.12)],
     [(6.96, 13.21), (6.96, 5.46)],
     [(10.09, 13.21), (10.09, 5.46)],
     [(5.59, 10.08), (12.24, 10.08)],
     [(4.41, 5.57), (13.34, 5.57)],
     [(7.47, 3.73), (3.63, 0.09)],
     [(9.89, 3.73), (12.83, 1.07)]],
    # 中
    [[(16.35, 10.54), (16.35, 4.79)],
     [(16.35, 10.27), (26.92, 10.27), (26.92, 4.91)],
     [(16.35, 5.77), (26.92, 5.77)],
     [(21.64, 13.60), (21.64, 0.09)]],
    # 航
    [[(32.75, 13.40), (31.97, 11.45)],
     ["arc", (31.97, 11.45), (31.60, 4.20), (29.81, 0.09)],
     [(31.97, 11.45), (34.90, 11.45), (34.90, 1.27), (33.92, 1.46)],
     [(32.94, 9.68), (33.53, 8.51)],
     [(32.94, 5.57), (33.53, 4.40)],
     [(29.62, 6.75), (35.88, 7.14)],
     [(38.82, 13.01), (39.40, 11.64)],
     [(36.08, 10.86), (42.14, 10.86)],
     ["arc", (37.45, 8.90), (37.20, 4.20), (35.88, 0.68)],
     [(37.45, 8.90), (40.19, 8.90), (40.19, 2.05), (41.16, 1.27),
      (42.73, 1.27), (42.85, 3.23)]],
    # 模
    [[(44.49, 10.08), (48.60, 10.08)],
     [(46.84, 13.60), (46.84, 0.09)],
     [(46.76, 9.49), (44.49, 3.42)],
     [(47.43, 7.73), (48.60, 6.16)],
     [(48.99, 12.03), (57.80, 12.03)],
     [(51.54, 13.60), (51.54, 10.54)],
     [(55.06, 13.60), (55.06, 10.54)],
     [(50.68, 10.39), (50.68, 5.30)],
     [(50.68, 10.39), (56.16, 10.39), (56.16, 5.30)],
     [(50.68, 7.84), (56.16, 7.84)],
     [(50.68, 5.38), (56.16, 5.38)],
     [(49.19, 3.73), (58.19, 3.73)],
     ["arc", (53.49, 5.18), (52.70, 2.40), (49.38, 0.09)],
     [(54.08, 2.83), (58.19, 0.29)]],
    # 队
    [[(60.99, 12.62), (60.99, 0.29)],
     [(60.99, 12.50), (65.03, 12.50), (63.07, 8.31)],
     ["arc", (63.07, 8.31), (65.00, 5.60), (63.30, 3.00)],
     ["arc", (68.35, 13.21), (67.30, 5.60), (63.07, 0.37)],
     ["arc", (68.55, 10.08), (69.70, 5.40), (72.66, 1.27)]],
]

cn_faces = []
for glyph in CN_GLYPHS:
    for stroke in glyph:
        if stroke[0] == "arc":
            p = [(CN_X0 + CN_SCALE * x, CN_Y0 + CN_SCALE * y) for x, y in stroke[1:]]
            cn_faces += path_faces([("A", p[0], p[1], p[2])], CN_W, caps=False)
        else:
            pts = [(CN_X0 + CN_SCALE * x, CN_Y0 + CN_SCALE * y) for x, y in stroke]
            cn_faces += poly_faces(pts, CN_W, caps=False)
cn_text = faces_to_solid(cn_faces, CN_H, z0)


# ---------------- English text: simple bold stroke font ----------------
def arc_pts(c, r, angles):
    return [(c[0] + r * math.cos(math.radians(t)),
             c[1] + r * math.sin(math.radians(t))) for t in angles]


def glyph_paths(ch, x0, x1, w):
    """stroke centre lines (paths), rings and dots of one letter in [x0, x1];
    y measured from the baseline"""
    a, b = x0 + w / 2, x1 - w / 2
    W = b - a
    xc = (a + b) / 2
    m = w / 2
    H = EN_CAP - w / 2
    h = EN_XH - w / 2
    paths, rings, dots = [], [], []
    if ch == "G":
        r = min(W, H - m) / 2
        c = (a + r, EN_CAP / 2)
        p = arc_pts(c, r, (48, 180, 338))
        yb = c[1] - 0.02 * r
        paths.append([("A", p[0], p[1], p[2]),
                      ("L", p[2], (p[2][0], yb)),
                      ("L", (p[2][0], yb), (p[2][0] - 0.5 * r, yb))])
    elif ch == "Z":
        paths.append([("L", (a, H), (b, H)), ("L", (b, H), (a, m)),
                      ("L", (a, m), (b, m))])
    elif ch == "A":
        paths.append([("L", (a, m), (xc, H)), ("L", (xc, H), (b, m))])
        paths.append([("L", (a + 0.27 * W, 0.3 * EN_CAP),
                       (b - 0.27 * W, 0.3 * EN_CAP))])
    elif ch == "o":
        rings.append(((xc, EN_XH / 2), min(W, h - m) / 2))
    elif ch == "e":
        r = min(W, h - m) / 2
        c = (xc, EN_XH / 2)
        p = arc_pts(c, r, (0, 155, 310))
        paths.append([("L", (c[0] - r, c[1]), p[0]),
                      ("A", p[0], p[1], p[2])])
    elif ch == "r":
        paths.append([("L", (a, m), (a, h))])
        paths.append([("A", (a, 0.5 * EN_XH), (a + 0.45 * W, h), (b, h - 0.15))])
    elif ch in "mn":
        k = 2 if ch == "m" else 1
        paths.append([("L", (a, m), (a, h))])
        step = W / k
        for i in range(k):
            s0 = a + i * step
            s1 = s0 + step
            ym = 0.55 * EN_XH
            paths.append([("A", (s0, ym), ((s0 + s1) / 2, h), (s1, ym)),
                          ("L", (s1, ym), (s1, m))])
    elif ch in "dg":
        r = min(W, h - m) / 2
        c = (b - r, EN_XH / 2)
        rings.append((c, r))
        if ch == "d":
            paths.append([("L", (b, m), (b, H))])
        else:
            yb = -EN_DESC + m
            paths.append([("L", (b, h), (b, 0.0)),
                          ("A", (b, 0.0), (xc, yb), (a, -0.25))])
    elif ch == "a":
        rb = 0.25 * EN_XH
        c = (b - rb - 0.05, m + rb)
        rings.append((c, rb))
        ys = 0.62 * EN_XH
        paths.append([("L", (b, m), (b, ys)),
                      ("A", (b, ys), (xc + 0.05 * W, h), (a + 0.08 * W, 0.8 * EN_XH))])
    elif ch == "l":
        paths.append([("L", (xc, m), (xc, H))])
    elif ch == "i":
        paths.append([("L", (xc, m), (xc, h))])
        dots.append(((xc, EN_XH + 0.85), w * 0.6))
    elif ch == "t":
        xs = a + 0.3 * W
        yk = 0.35 * EN_XH
        paths.append([("L", (xs, 0.85 * EN_CAP), (xs, yk)),
                      ("A", (xs, yk), (xs + 0.45 * (b - xs), m + 0.05),
                       (b, m + 0.2))])
        paths.append([("L", (a, h), (b, h))])
    return paths, rings, dots


# letter boxes (x range, mm) measured along the baseline
EN_LETTERS = [
    ("G", -35.10, -30.68), ("Z", -30.20, -25.82),
    ("A", -23.35, -18.44), ("e", -18.21, -14.78), ("r", -14.54, -12.73),
    ("o", -12.54, -8.69), ("m", -8.69, -3.21), ("o", -3.21, 0.45),
    ("d", 0.45, 4.31), ("e", 4.50, 7.64), ("l", 8.02, 8.78),
    ("l", 9.40, 10.21), ("i", 10.78, 11.59), ("n", 12.16, 14.97),
    ("g", 15.78, 19.16),
    ("t", 21.73, 23.73), ("e", 23.92, 26.68), ("a", 27.11, 29.87),
    ("m", 30.68, 35.63),
]

en_faces = []
for ch, xa, xb in EN_LETTERS:
    paths, rings, dots = glyph_paths(ch, xa, xb, EN_W)
    for p in paths:
        segs = []
        for s in p:
            if s[0] == "L":
                segs.append(("L", (s[1][0], s[1][1] + EN_BASE),
                             (s[2][0], s[2][1] + EN_BASE)))
            else:
                segs.append(("A", (s[1][0], s[1][1] + EN_BASE),
                             (s[2][0], s[2][1] + EN_BASE),
                             (s[3][0], s[3][1] + EN_BASE)))
        en_faces += path_faces(segs, EN_W)
    for c, r in rings:
        en_faces.append(ring_face((c[0], c[1] + EN_BASE), r, EN_W))
    for c, r in dots:
        en_faces.append(dot_face((c[0], c[1] + EN_BASE), r))
en_text = faces_to_solid(en_faces, EN_H, z0)

body = body.union(cq.Workplane("XY").add(cn_text)).union(
    cq.Workplane("XY").add(en_text))
result = body.union(bolt_top, clean=False)
